import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 370.0            # overall length (X)
W = 122.0            # overall depth of the straight body (Y)
T = 11.5             # overall thickness (Z)
R_CORNER = 10.0      # outer vertical corner radius

# front bulge (towards -Y)
BULGE_XC = -5.5      # bulge centre (X)
BULGE_HALF = 102.5   # half span of the bulge along X
BULGE_ANG = 12.5     # flank angle of the bulge (deg)
BULGE_DEPTH = 17.4   # how far the bulge sticks out beyond the straight front edge
KINK_R = 15.0        # radius where the bulge leaves the straight edge

# pocket
RIM_FRONT = 9.8      # front rim width (also along the bulge)
RIM_BACK = 10.5      # back rim width
RIM_SIDE = 15.0      # end rim width (carries the slots)
POCKET_D = 8.3       # pocket depth from top face

# back notch + floor recess
NOTCH_W = 21.5       # notch width (X)
NOTCH_Y0 = 0.0       # recess starts at this Y and runs out through the back wall
RECESS_D = 1.0       # recess depth below the pocket floor

# end slots and holes
SLOT_W = 6.0
SLOT_LEN = 87.0
BIG_HOLE_D = 5.5
BIG_HOLE_Y = 51.0
RIM_HOLE_D = 3.0
FLOOR_HOLE_D = 2.2
CSK_D = 5.5          # countersink diameter on the underside
CSK_ANG = 90.0

FLOOR = T - POCKET_D
X_END = L / 2 - RIM_SIDE / 2          # X of slots / big holes
X_WALL = L / 2 - RIM_SIDE             # X of the pocket end walls

# ---------------- helpers ----------------


def rounded_polygon(pts, radii):
    """Closed wire through pts (CCW) with a tangent fillet arc of radius
    radii[i] at every vertex i (0 -> sharp corner)."""
    n = len(pts)
    corner = []
    for i in range(n):
        p = pts[i]
        a = pts[i - 1]
        b = pts[(i + 1) % n]
        r = radii[i]
        d1 = (p[0] - a[0], p[1] - a[1])
        l1 = math.hypot(*d1)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (b[0] - p[0], b[1] - p[1])
        l2 = math.hypot(*d2)
        d2 = (d2[0] / l2, d2[1] / l2)
        if r <= 0:
            corner.append((p, p, None))
            continue
        cosphi = max(-1.0, min(1.0, d1[0] * d2[0] + d1[1] * d2[1]))
        phi = math.acos(cosphi)                 # turning angle
        t = r * math.tan(phi / 2.0)             # tangent length
        s = (p[0] - d1[0] * t, p[1] - d1[1] * t)
        e = (p[0] + d2[0] * t, p[1] + d2[1] * t)
        bis = (d2[0] - d1[0], d2[1] - d1[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        k = r / math.cos(phi / 2.0) - r
        m = (p[0] + bis[0] * k, p[1] + bis[1] * k)
        corner.append((s, e, m))
    wp = cq.Workplane("XY").moveTo(*corner[0][1])
    for i in range(1, n + 1):
        s, e, m = corner[i % n]
        wp = wp.lineTo(*s)
        if m is not None:
            wp = wp.threePointArc(m, e)
    return wp.close()


def bulge_radius():
    # radius of the bottom arc so that the bulge reaches BULGE_DEPTH
    th = math.radians(BULGE_ANG)
    h = BULGE_HALF * math.tan(th)
    return (h - BULGE_DEPTH) / (1.0 / math.cos(th) - 1.0)


def outline_pts():
    h = BULGE_HALF * math.tan(math.radians(BULGE_ANG))
    pts = [
        (-L / 2, -W / 2),
        (BULGE_XC - BULGE_HALF, -W / 2),
        (BULGE_XC, -W / 2 - h),
        (BULGE_XC + BULGE_HALF, -W / 2),
        (L / 2, -W / 2),
        (L / 2, W / 2),
        (-L / 2, W / 2),
    ]
    radii = [R_CORNER, KINK_R, bulge_radius(), KINK_R, R_CORNER, R_CORNER, R_CORNER]
    return pts, radii


# ---------------- body ----------------
pts, radii = outline_pts()
body = rounded_polygon(pts, radii).extrude(T)

# pocket: inward offset of the outline (constant front rim, also along the
# bulge), clipped by the end rims and the back rim -> square pocket corners
pocket_prof = (
    rounded_polygon(pts, radii)
    .offset2D(-RIM_FRONT, "intersection")
    .extrude(POCKET_D + 1.0)
    .translate((0, 0, FLOOR))
)
clip_y0 = -W / 2 - BULGE_DEPTH - 5.0
clip_y1 = W / 2 - RIM_BACK
clip = (
    cq.Workplane("XY")
    .box(2 * X_WALL, clip_y1 - clip_y0, POCKET_D + 2.0, centered=(True, False, False))
    .translate((0, clip_y0, FLOOR))
)
body = body.cut(pocket_prof.intersect(clip))

# back notch through the wall + shallow recess in the floor (same width)
notch = (
    cq.Workplane("XY")
    .box(NOTCH_W, W / 2 - NOTCH_Y0 + 5.0, T, centered=(True, False, False))
    .translate((0, NOTCH_Y0, FLOOR - RECESS_D))
)
body = body.cut(notch)

# end slots (through)
for sx in (-1, 1):
    slot = (
        cq.Workplane("XY")
        .center(sx * X_END, 0)
        .slot2D(SLOT_LEN, SLOT_W, angle=90)
        .extrude(T + 2)
        .translate((0, 0, -1))
    )
    body = body.cut(slot)

# big corner holes on the end rims (plain through holes)
big_pts = [(sx * X_END, sy * BIG_HOLE_Y) for sx in (-1, 1) for sy in (-1, 1)]
body = (
    body.faces("<Z").workplane(origin=(0, 0, 0))
    .pushPoints([(x, -y) for x, y in big_pts])   # bottom plane: local y = -Y
    .hole(BIG_HOLE_D)
)

# small screw holes on the front / back rims (countersunk from below)
yb = W / 2 - RIM_BACK / 2
yf = -W / 2 + RIM_FRONT / 2
rim_pts = [
    (-X_WALL, yb), (-85.0, yb), (-NOTCH_W / 2 - 4.5, yb), (NOTCH_W / 2 + 4.5, yb),
    (84.5, yb), (X_WALL, yb),
    (-X_WALL, yf), (BULGE_XC - BULGE_HALF, yf),
    (BULGE_XC, -W / 2 - BULGE_DEPTH + RIM_FRONT / 2),
    (BULGE_XC + BULGE_HALF, yf), (X_WALL, yf),
]

# small mounting holes in the pocket floor (countersunk from below)
floor_pts = [
    (-141.8, 20.0), (-74.6, 17.0), (-116.0, 0.4), (-54.7, -6.6), (-158.7, -24.2),
    (-5.4, -14.4), (-4.8, -34.9), (1.9, -54.0),
    (54.4, 15.6), (43.1, -6.6), (102.3, 0.1), (135.7, 20.9),
]

body = (
    body.faces("<Z").workplane(origin=(0, 0, 0))
    .pushPoints([(x, -y) for x, y in rim_pts])
    .cskHole(RIM_HOLE_D, CSK_D, CSK_ANG)
)
body = (
    body.faces("<Z").workplane(origin=(0, 0, 0))
    .pushPoints([(x, -y) for x, y in floor_pts])
    .cskHole(FLOOR_HOLE_D, CSK_D, CSK_ANG)
)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
